import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
OD = 100.0            # outer diameter
H = 20.0              # overall height
MINOR_D = 80.6        # thread crest (minor) diameter of the threaded bore
MAJOR_D = 84.8        # thread root (major) diameter
BORE_DEPTH = 13.4     # depth of threaded bore from top face
HOLE_D = 60.7         # through hole in the bottom web
OUT_FILLET = 7.4      # outer bottom edge round
IN_FILLET = 6.0       # hole bottom edge round

# internal thread: right hand, 60 deg flanks, narrow crest / wide root
PITCH = 4.65          # thread pitch
CREST_W = 0.75        # axial width of the crest land (at the minor diameter)
FLANK_ANGLE = 30.0    # flank angle from the radial direction (60 deg included)
PHASE_ANG = 135.0     # polar angle (deg, +X towards +Y) at which ...
PHASE_Z = 6.95        # ... a crest centre lies at this height
START_SINK = 0.5      # the groove starts below the shoulder; it is trimmed at the shoulder plane
END_ANG = 309.0       # polar angle where the groove ends (breaking through the top face)

R_o = OD / 2.0
R_min = MINOR_D / 2.0
R_maj = MAJOR_D / 2.0
R_h = HOLE_D / 2.0
z_s = H - BORE_DEPTH          # height of the shoulder (top of bottom web)

# ---------------- ring: revolved section ----------------
pts = [
    (R_h, 0.0),
    (R_o, 0.0),
    (R_o, H),
    (R_min, H),
    (R_min, z_s),
    (R_h, z_s),
]
body = (cq.Workplane("XZ").polyline(pts).close()
        .revolve(360, (0, 0, 0), (0, 1, 0)))

# rounded underside: large round on the outer and on the hole edge
body = body.faces("<Z").edges(cq.selectors.RadiusNthSelector(1)).fillet(OUT_FILLET)
body = body.faces("<Z").edges(cq.selectors.RadiusNthSelector(0)).fillet(IN_FILLET)


# ---------------- helical thread groove ----------------
def helical_solid(pitch, height, z_start, section):
    """Right hand helical sweep of a closed (radius, dz) section: ruled faces spanned
    between helices through the section corners, closed by two planar end caps."""
    helices = [cq.Wire.makeHelix(pitch, height, r, center=cq.Vector(0, 0, z_start + dz)).Edges()[0]
               for (r, dz) in section]
    n = len(helices)
    faces = [cq.Face.makeRuledSurface(helices[i], helices[(i + 1) % n]) for i in range(n)]
    faces.append(cq.Face.makeFromWires(
        cq.Wire.makePolygon([e.startPoint() for e in helices], close=True)))
    faces.append(cq.Face.makeFromWires(
        cq.Wire.makePolygon([e.endPoint() for e in helices], close=True)))
    return cq.Solid.makeSolid(cq.Shell.makeShell(faces))


depth = R_maj - R_min
tan_f = math.tan(math.radians(FLANK_ANGLE))
groove_w = PITCH - CREST_W                    # groove width at the minor diameter
root_w = groove_w - 2.0 * tan_f * depth       # flat at the thread root
eps = 0.3                                     # groove flanks continue slightly inside the bore
r_in = R_min - eps
hw_in = groove_w / 2.0 + tan_f * eps
section = [
    (r_in, -hw_in),
    (R_maj, -root_w / 2.0),
    (R_maj, root_w / 2.0),
    (r_in, hw_in),
]


# groove centre height: zc(theta) = zc0 + PITCH * (theta - PHASE_ANG) / 360  (+ k * PITCH)
zc0 = PHASE_Z - PITCH / 2.0
# start on the lowest turn just below the shoulder; the part of the groove below the
# shoulder plane is trimmed away, so the thread runs out onto the shoulder
z_start = z_s - START_SINK - hw_in
start_ang = PHASE_ANG + (z_start - zc0) * 360.0 / PITCH
# end at END_ANG on the turn that breaks through the top face
z_end = zc0 + PITCH * (END_ANG - PHASE_ANG) / 360.0
z_end -= PITCH * math.floor((z_end - z_start) / PITCH)
while z_end - groove_w / 2.0 < H:
    z_end += PITCH
z_end -= PITCH                                 # last turn whose lower edge is still below H
groove = helical_solid(PITCH, z_end - z_start, z_start, section)
groove = groove.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), start_ang % 360.0)
keep = cq.Workplane("XY").workplane(offset=z_s).circle(R_maj + 1.0).extrude(H + 5.0 - z_s)
groove = keep.val().intersect(groove)

# Cut the groove.  The ring is a solid of revolution, so turning it about its axis does
# not change it; only its seam moves.  Pick a seam position for which the boolean is
# clean (checked through the removed volume).
ring = body.val()
expect = 0.5 * groove.Volume()
cut = None
for seam in (45.0, 60.0, 30.0, 90.0, 120.0, 150.0, 0.0, 180.0, 210.0, 240.0, 270.0, 300.0, 330.0):
    cand = ring.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), seam).cut(groove).clean()
    if (len(cand.Solids()) == 1 and cand.isValid()
            and ring.Volume() - cand.Volume() > expect):
        cut = cand
        break
if cut is None:
    cut = ring.cut(groove)
body = cq.Workplane("XY").add(cut)

result = body
